import math
import cadquery as cq

# =====================================================================
#  Drive unit: hollow drum (axis X) + cut-away gear housing (axis Y)
#  All dimensions in mm.  Drum axis = X axis (Y=0, Z=0).
# =====================================================================

# ---------------- main drum ----------------
R_MAIN = 45.5                 # drum outer radius
X_MAIN0, X_MAIN1 = 89.0, 142.0
R_FACE = 43.0                 # thin face plate on the +X end
X_FACE1 = 144.3
R_BORE = 21.0                 # through bore
R_TUBE = 25.5                 # short spigot on the +X face
X_TUBE1 = 149.5
R_GROOVE = 41.0               # groove ring on the face plate
R_RECESS = 36.5               # annular recess around the spigot
RECESS_DEPTH = 4.0
PAD_X0, PAD_X1 = 97.0, 107.0  # raised pads on the -Y side of the drum

# square flange at the back of the drum
FL_X0, FL_X1 = 88.0, 93.0
FL_Y0, FL_Y1 = -42.0, 43.0
FL_Z0, FL_Z1 = -43.0, 42.0
FL_R = 10.0

# side lobe with four pins and the terminal stud (on +Y side)
PIN_RC = 48.5
PIN_R = 6.0
PIN_ANGLES = [27.0, 45.0, -27.0, -45.0]
LOBE_X0, LOBE_X1 = 88.0, 111.0
LOBE_OFF = 7.0
STUD_Y = 56.0
STUD_R = 6.2
STUD_HEX_R = 8.2
STUD_X1 = 150.0
SB_X0, SB_X1 = 104.5, 139.0   # stud base block
SB_Y1 = 66.0
SB_Z = 12.5
SB_CHAMFER = 4.0

# ---------------- gear housing (axis along Y) ----------------
GH_X, GH_Z = 44.0, -1.0       # centre of the round features
GH_Y0, GH_Y1 = 46.0, 58.0     # main back disc
GH_XMIN = 2.0
GH_PROF = [(GH_XMIN, -29.0), (GH_XMIN, 27.5), (6.4, 34.4), (20.5, 37.6), (43.6, 43.4),
           (67.0, 44.75), (76.0, 44.75), (89.0, 32.0), (89.0, -32.0), (76.0, -44.75),
           (69.0, -44.75), (43.6, -42.6), (20.5, -37.2), (6.4, -34.4)]
GH_R_CAP = 42.4               # raised round cap on +Y face
GH_Y2 = 61.0
CAP_RECESS_R = 21.0
RING_RO, RING_RI = 34.0, 31.0  # cut-open ring wall in front of the disc
RING_Y0 = 24.0
RING_PIN_RC = 25.3
RING_PIN_R = 5.0
RING_ANGLES = [36, 63, 90, 118, -36, -63, -90, -118]
SHAFT_R = 14.0
SHAFT_Y = 38.0
SHAFT_X0, SHAFT_X1 = 12.5, 57.0
STUB_R, STUB_RI = 9.4, 5.0
STUB_Y = 52.0

# adapter block between housing and drum
AD_X0, AD_X1 = 70.0, 88.0
AD_Y0, AD_Y1 = 4.0, 46.0
AD_Z0, AD_Z1 = -46.0, 46.0
AD_R = 46.5

# top saddle block
TB_PTS = [(54.0, 48.0), (84.0, 48.0), (84.0, 7.5), (57.0, 34.0), (54.0, 34.0)]
TB_Z0, TB_Z1 = 34.0, 52.0
TB_FILLET = 14.0
TB_FILLET_Y = 5.0
TB_STEP_X, TB_STEP_Z = 70.0, 44.0


# ---------------- helpers ----------------
def cyl_x(r, x0, x1, y=0.0, z=0.0):
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).center(y, z)
            .circle(r).extrude(x1 - x0))


def cyl_y(r, y0, y1, x=0.0, z=0.0):
    # XZ workplane normal is -Y, so extrude negative
    return (cq.Workplane("XZ", origin=(0, y0, 0)).center(x, z)
            .circle(r).extrude(-(y1 - y0)))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


class EdgeSel(cq.Selector):
    """select objects whose centre satisfies a predicate"""
    def __init__(self, pred):
        self.pred = pred

    def filter(self, objs):
        return [o for o in objs if self.pred(o.Center())]


def pin_yz(a, rc=PIN_RC):
    return rc * math.cos(math.radians(a)), rc * math.sin(math.radians(a))


# =====================================================================
#  Drum
# =====================================================================
drum = cyl_x(R_MAIN, X_MAIN0, X_MAIN1)
drum = drum.union(cyl_x(R_FACE, X_MAIN1, X_FACE1))
drum = drum.union(cyl_x(R_TUBE, X_FACE1, X_TUBE1))
groove = cyl_x(R_GROOVE + 0.6, X_FACE1 - 0.8, X_FACE1 + 1).cut(
    cyl_x(R_GROOVE - 0.6, X_FACE1 - 1, X_FACE1 + 2))
drum = drum.cut(groove)
drum = drum.cut(cyl_x(R_RECESS, X_FACE1 - RECESS_DEPTH, X_FACE1 + 1).cut(
    cyl_x(R_TUBE, X_FACE1 - RECESS_DEPTH - 1, X_FACE1 + 2)))
# small notch in the rim at the top of the face
drum = drum.cut(box(X_FACE1 - 6, X_FACE1 + 1, -1.5, 1.5, R_FACE - 3, R_MAIN + 1))

# thin rounded-square flange at the back of the drum
flange = (cq.Workplane("YZ", origin=(FL_X0, 0, 0))
          .center((FL_Y0 + FL_Y1) / 2, (FL_Z0 + FL_Z1) / 2)
          .rect(FL_Y1 - FL_Y0, FL_Z1 - FL_Z0).extrude(FL_X1 - FL_X0)
          .edges("|X").fillet(FL_R))
drum = drum.union(flange)

# side lobe: rounded hull around the four pins and the stud
pts = [(0.0, 0.0), pin_yz(45.0), pin_yz(27.0), (STUD_Y, 0.0), pin_yz(-27.0), pin_yz(-45.0)]
lobe = (cq.Workplane("YZ", origin=(LOBE_X0, 0, 0)).polyline(pts).close()
        .offset2D(LOBE_OFF).extrude(LOBE_X1 - LOBE_X0))
drum = drum.union(lobe)

# pins, with clearance grooves along the drum in front of each pin
for a in PIN_ANGLES:
    ya, za = pin_yz(a)
    drum = drum.cut(cyl_x(PIN_R + 0.5, LOBE_X1, X_FACE1 + 1, ya, za))
    drum = drum.union(cyl_x(PIN_R - 1.8, LOBE_X1 - 1, LOBE_X1 + 3.5, ya, za))
    drum = drum.union(cyl_x(PIN_R - 1.8, FL_X0 - 8, FL_X0 + 1, ya, za))

# stud base block + terminal stud with chamfered end
sb_box = box(SB_X0, SB_X1, STUD_Y, SB_Y1, -SB_Z, SB_Z).edges(
    EdgeSel(lambda c: abs(c.y - SB_Y1) < 0.1 and abs(abs(c.z) - SB_Z) < 0.1)).chamfer(SB_CHAMFER)
sb = cyl_x(11.0, SB_X0, SB_X1, STUD_Y, 0).union(sb_box)
sb = sb.union(box(SB_X0, SB_X0 + 8, STUD_Y, SB_Y1 + 1.2, -SB_Z, SB_Z))
drum = drum.union(sb)
stud = cyl_x(STUD_HEX_R, SB_X1 - 1, STUD_X1, STUD_Y, 0).faces(">X").chamfer(STUD_HEX_R - STUD_R)
drum = drum.union(stud)

# small ear on the lobe
drum = drum.union(box(92.0, 104.0, 45.0, 58.0, -4.0, 4.0))

# raised pads on the -Y side of the drum near the flange
for zc in (30.0, -31.0):
    pad = cyl_x(R_MAIN + 2.2, PAD_X0, PAD_X1).intersect(
        box(PAD_X0, PAD_X1, -60, -5, zc - 11, zc + 11))
    drum = drum.union(pad)

# =====================================================================
#  Gear housing
# =====================================================================
gh = (cq.Workplane("XZ", origin=(0, GH_Y0 + 2.0, 0)).polyline(GH_PROF).close()
      .extrude(-(GH_Y1 - GH_Y0 - 2.0)))
# inset lip on the -Y side (stepped outline seen from the front)
lip = (cq.Workplane("XZ", origin=(0, GH_Y0, 0)).polyline(GH_PROF).close()
       .offset2D(-3.0).extrude(-2.5))
gh = gh.union(lip)
# raised round cap on the +Y face with a central recess
gh = gh.union(cyl_y(GH_R_CAP, GH_Y1 - 1, GH_Y2, GH_X, GH_Z))
gh = gh.cut(cyl_y(CAP_RECESS_R, GH_Y2 - 8, GH_Y2 + 1, GH_X, GH_Z))
# circular recess on the -Y face inside the ring
gh = gh.cut(cyl_y(37.0, GH_Y0 - 1, GH_Y0 + 5, GH_X, GH_Z).intersect(
    box(0, 72, GH_Y0 - 2, GH_Y0 + 6, -60, 60)))
# small lug on top
gh = gh.union(box(40.0, 51.0, 49.0, 58.0, 40.0, 45.75))

# cut-open ring wall (open towards +X and around the shaft)
ring = cyl_y(RING_RO, RING_Y0, GH_Y0 + 1, GH_X, GH_Z).cut(
    cyl_y(RING_RI, RING_Y0 - 1, GH_Y0 + 2, GH_X, GH_Z))
ring = ring.cut(box(72, 100, RING_Y0 - 2, GH_Y0 + 3, -60, 60))
ring = ring.cut(box(0, 30, RING_Y0 - 2, GH_Y0 + 3, -17, 17))
gh = gh.union(ring)

# inner shaft along X with domed end + hollow stub on the end wall
shaft = cyl_x(SHAFT_R, SHAFT_X0, SHAFT_X1, SHAFT_Y, 0)
shaft = shaft.union(cq.Workplane("XY").sphere(SHAFT_R).translate((SHAFT_X1, SHAFT_Y, 0)))
stub = cyl_x(STUB_R, 1.25, 12.0, STUB_Y, 0).cut(cyl_x(STUB_RI, 0, 8.0, STUB_Y, 0))
gh = gh.union(shaft).union(stub)

# ring of pins (axis along Y)
for a in RING_ANGLES:
    px = GH_X + RING_PIN_RC * math.cos(math.radians(a))
    pz = RING_PIN_RC * math.sin(math.radians(a))
    pin = cyl_y(RING_PIN_R, RING_Y0, GH_Y0 + 6, px, pz).faces("<Y").chamfer(0.8)
    pin = pin.cut(cyl_y(RING_PIN_R - 1.6, RING_Y0 - 1, RING_Y0 + 1.0, px, pz))
    gh = gh.union(pin)

# adapter between housing and drum: a middle web and a lower block, both
# rounded like the drum (upper part is carried by the saddle)
ad = box(AD_X0 + 2, AD_X1, AD_Y0, AD_Y1, -14.0, 14.0)
ad = ad.union(box(AD_X0, AD_X1, AD_Y0, AD_Y1, AD_Z0, -28.4))
ad = ad.intersect(cyl_x(AD_R, AD_X0, AD_X1))
ad = ad.cut(box(AD_X0 + 4, AD_X1 - 2, AD_Y0 - 1, AD_Y0 + 2.5, -10.0, 10.0))
gh = gh.union(ad)

# =====================================================================
#  Top saddle: trapezoid plan with rounded top edges
# =====================================================================
tb = (cq.Workplane("XY", origin=(0, 0, TB_Z0)).polyline(TB_PTS).close()
      .extrude(TB_Z1 - TB_Z0))
# round the top edges on the +X and +Y sides
tb = tb.edges(EdgeSel(lambda c: abs(c.z - TB_Z1) < 0.1 and abs(c.x - TB_PTS[1][0]) < 0.1)).fillet(TB_FILLET)
tb = tb.edges(EdgeSel(lambda c: c.z > TB_Z1 - TB_FILLET - 0.1 and abs(c.y - TB_PTS[0][1]) < 0.1
                      and c.x < TB_PTS[1][0] - TB_FILLET + 0.1)).fillet(TB_FILLET_Y)
# the part of the saddle over the housing only sits on top of the housing
tb = tb.cut(box(0, TB_STEP_X, 0, 60, TB_Z0 - 1, TB_STEP_Z))
try:
    tb = tb.edges(EdgeSel(lambda c: abs(c.z - TB_Z1) < 0.1 and abs(c.x - TB_PTS[0][0]) < 0.1)).fillet(4.0)
except Exception:
    pass

result = drum.union(gh).union(tb)
# through bore
result = result.cut(cyl_x(R_BORE, X_MAIN0 - 20, X_TUBE1 + 1))
